import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Close-coupled floor-standing WC: pedestal + bowl, seat & lid, cistern (tank)
# X = width (symmetric), Y = depth (front of seat at Y=0, tank at +Y), Z = up
# ---------------------------------------------------------------------------

# --- overall ---------------------------------------------------------------
RIM_Z = 389.0            # top of bowl rim / deck
# --- seat & lid ------------------------------------------------------------
SEAT_YC = 207.0          # Y of widest point of seat
SEAT_A = 179.0           # half width of seat
SEAT_BF = 207.0          # front half-length
SEAT_BB = 335.0          # back half-length (truncated at SEAT_BACK)
SEAT_NB = 1.6            # exponent of back half (straight-ish flanks)
SEAT_BACK = 424.0
SEAT_GAP = 5.0           # gap between rim and seat (buffers)
SEAT_T = 19.0            # seat ring thickness
LID_T = 21.0             # lid thickness
LID_INSET = 10.0         # chamfer-like draft of the lid edge
SEAT_CORNER_R = 32.0     # plan radius at the hinge-side corners
LID_GROOVE_L = 70.0      # length of the parting groove on the lid
# --- bowl ------------------------------------------------------------------
BOWL_A = 171.5
BOWL_BOTTOM_Z = 222.0
# inner bowl: (yc, a, bf, bb, z) sections from above the rim down to the sump
BOWL_CAVITY = [
    (200.0, 126.0, 160.0, 178.0, RIM_Z + 2),
    (200.0, 122.0, 155.0, 172.0, RIM_Z - 25),
    (200.0, 100.0, 128.0, 140.0, 320.0),
    (215.0, 50.0, 55.0, 70.0, 262.0),
]
SEAT_HOLE = (205.0, 116.0, 150.0, 152.0)   # yc, a, bf, bb of seat-ring opening
# --- pedestal (foot) -------------------------------------------------------
PED_HW_BOT = 113.5
PED_HW_TOP = 91.0
PED_Y0_BOT = 106.0
PED_Y0_TOP = 123.0
PED_Y1_BOT = 428.0       # back of main trunk at floor
PED_Y1_TOP = 405.0       # back of main trunk at top
PED_RF_BOT = 98.0
PED_RF_TOP = 82.0
PED_RB = 26.0
FLANGE_Y1 = 444.0        # foot flange reaches back to here
FLANGE_H = 30.0
# --- spine / trap at the back ----------------------------------------------
SPINE_Y1 = 447.0         # back face of the trap column
SPINE_HW = 58.0          # half width of the trap body at its back face
SPINE_FRONT_HW = 88.0    # half width where it leaves the foot
RIB_R = 16.0
WEB_HW = 20.0            # half thickness of the trapway web under the deck
SPINE_TOP_Z = 235.0
TRAP_END = (541.0, 329.0)
# --- neck / deck -----------------------------------------------------------
DECK_HW = 125.0
DECK_Y1 = 623.0
DECK_FRONT_Y1 = 535.0    # full-width part of the deck runs under the tank front
DECK_BACK_HW = 75.0
DECK_T = 16.0
NECK_BACK_TOP = 410.0    # back edge of the wide neck under the deck
NECK_TOP_HW = 118.0      # flare half width where the neck meets the deck
NECK_HW = 89.0           # neck half width where it rises out of the foot
# --- outlet horn -----------------------------------------------------------
HORN_D = 101.0
HORN_Z = 180.0
HORN_Y1 = 518.0
# --- tank ------------------------------------------------------------------
TANK_Y0 = 479.0
TANK_Y1 = 642.0
TANK_Z0 = 398.0
TANK_Z1 = 719.0
TANK_HW_TOP = 165.0
TANK_HW_BOT = 148.0
TANK_RF = 72.0           # front corner radius (plan)
TANK_RB = 12.0           # back corner radius (plan)
LID_Z1 = 759.0
LID_EDGE_R = 18.0
# --- flush-valve housing under tank ----------------------------------------
VALVE_D = 92.0
VALVE_Y = 562.0
VALVE_Z0 = 334.0


def egg_pts(yc, a, bf, bb, nf=2.4, nb=2.0, n=20):
    """Closed egg-shaped outline: super-ellipse front, ellipse back."""
    pts = []
    for i in range(n):
        t = math.pi / 2 + 2 * math.pi * i / n   # seam at the back
        c, s = math.cos(t), math.sin(t)
        if s >= 0:   # back half (+Y)
            e, b = nb, bb
        else:
            e, b = nf, bf
        x = a * math.copysign(abs(c) ** (2.0 / e), c)
        y = yc + b * math.copysign(abs(s) ** (2.0 / e), s)
        pts.append((x, y))
    return pts


def egg_wire(yc, a, bf, bb, z, nf=2.4, nb=2.0, n=20):
    pts = [cq.Vector(x, y, z) for x, y in egg_pts(yc, a, bf, bb, nf, nb, n)]
    # same (angular) parameterisation for every section -> clean lofts
    e = cq.Edge.makeSpline(pts, periodic=True, parameters=[i / n for i in range(n + 1)])
    return cq.Wire.assembleEdges([e])


def egg_solid(yc, a, bf, bb, z0, h, nf=2.4, nb=2.0):
    w = egg_wire(yc, a, bf, bb, z0, nf, nb)
    f = cq.Face.makeFromWires(w)
    return cq.Solid.extrudeLinear(f, cq.Vector(0, 0, h))


def rrect_wire(hw, y0, y1, rf, rb, z):
    """Rounded rectangle in plan, front (low Y) corners rf, back corners rb."""
    V = cq.Vector
    k = math.sqrt(0.5)
    edges = [
        cq.Edge.makeLine(V(-hw + rf, y0, z), V(hw - rf, y0, z)),
        cq.Edge.makeThreePointArc(V(hw - rf, y0, z),
                                  V(hw - rf + rf * k, y0 + rf - rf * k, z),
                                  V(hw, y0 + rf, z)),
        cq.Edge.makeLine(V(hw, y0 + rf, z), V(hw, y1 - rb, z)),
        cq.Edge.makeThreePointArc(V(hw, y1 - rb, z),
                                  V(hw - rb + rb * k, y1 - rb + rb * k, z),
                                  V(hw - rb, y1, z)),
        cq.Edge.makeLine(V(hw - rb, y1, z), V(-hw + rb, y1, z)),
        cq.Edge.makeThreePointArc(V(-hw + rb, y1, z),
                                  V(-hw + rb - rb * k, y1 - rb + rb * k, z),
                                  V(-hw, y1 - rb, z)),
        cq.Edge.makeLine(V(-hw, y1 - rb, z), V(-hw, y0 + rf, z)),
        cq.Edge.makeThreePointArc(V(-hw, y0 + rf, z),
                                  V(-hw + rf - rf * k, y0 + rf - rf * k, z),
                                  V(-hw + rf, y0, z)),
    ]
    return cq.Wire.assembleEdges(edges)


def rrect_pts(hw, y0, y1, rf, rb, nb=2, nab=2, ns=3, naf=3, nf=2):
    """Points around a plan rounded rectangle (front corners rf, back corners rb),
    starting at the back centre; fixed counts per segment so sections loft cleanly."""
    pts = []

    def line(p, q, n):
        for i in range(n):
            t = i / n
            pts.append((p[0] + (q[0] - p[0]) * t, p[1] + (q[1] - p[1]) * t))

    def arc(c, r, a0, a1, n):
        for i in range(n):
            a = math.radians(a0 + (a1 - a0) * i / n)
            pts.append((c[0] + r * math.cos(a), c[1] + r * math.sin(a)))

    line((0, y1), (-hw + rb, y1), nb)
    arc((-hw + rb, y1 - rb), rb, 90, 180, nab)
    line((-hw, y1 - rb), (-hw, y0 + rf), ns)
    arc((-hw + rf, y0 + rf), rf, 180, 270, naf)
    line((-hw + rf, y0), (0, y0), nf)
    line((0, y0), (hw - rf, y0), nf)
    arc((hw - rf, y0 + rf), rf, 270, 360, naf)
    line((hw, y0 + rf), (hw, y1 - rb), ns)
    arc((hw - rb, y1 - rb), rb, 0, 90, nab)
    line((hw - rb, y1), (0, y1), nb)
    return pts


TANK_PTS = (6, 2, 4, 3, 2)      # spline points per segment: back, back arc, side, front arc, front
PED_PTS = (4, 3, 10, 4, 3)


def chord_params(pts2d):
    """Normalised cumulative chord length of a closed point loop (len + 1 values)."""
    d = [0.0]
    for i in range(1, len(pts2d) + 1):
        d.append(d[-1] + math.dist(pts2d[i - 1], pts2d[i % len(pts2d)]))
    return [v / d[-1] for v in d]


def smooth_rrect_wire(hw, y0, y1, rf, rb, z, counts=TANK_PTS, ref=None):
    """Rounded rectangle as one smooth periodic spline (no tangent seams).
    Sections of one loft share the parameterisation of `ref` so rulings stay straight."""
    pts2d = rrect_pts(hw, y0, y1, rf, rb, *counts)
    params = chord_params(rrect_pts(*ref, *counts) if ref else pts2d)
    pts = [cq.Vector(x, y, z) for x, y in pts2d]
    return cq.Wire.assembleEdges([cq.Edge.makeSpline(pts, periodic=True, parameters=params)])


def safe_fillet(wp, select, r):
    """Fillet selected edges; keep the original if OCC fails or returns a bad solid.
    `select` is an edge selector or a function workplane -> workplane of edges."""
    try:
        sel = select(wp) if callable(select) else wp.edges(select)
        out = sel.fillet(r)
        v0, v1 = wp.val().Volume(), out.val().Volume()
        if out.val().isValid() and abs(v1 - v0) < 0.05 * v0:
            return out
    except Exception:
        pass
    return wp


def fuse(a, b):
    """Boolean union that falls back to a fuzzy union if OCC silently drops material
    (a correct union is one valid solid at least as large as the larger operand)."""
    def vol(w):
        return sum(x.Volume() for x in w.solids().vals())
    va, vb = vol(a), vol(b)
    first = None
    for kw in ({}, {"tol": 1e-4}, {"tol": 1e-3}):
        try:
            r = a.union(b, **kw)
        except Exception:
            continue
        first = first or r
        vr = vol(r)
        if (r.solids().size() == 1 and r.val().isValid()
                and vr > max(va, vb) + 1.0 and vr <= va + vb + 1.0):
            return r
    return first if first is not None else a


def loft(wires, ruled=True):
    return cq.Workplane("XY").add(cq.Solid.makeLoft(wires, ruled))


def trap_profile(y_front, z_bot, z_top, dy=0.0):
    """Side (YZ) outline of the back of the pan: vertical trap column,
    concave sweep up to the underside of the deck."""
    ys, zt = SPINE_Y1 + dy, SPINE_TOP_Z
    return (
        cq.Workplane("YZ")
        .moveTo(y_front, z_bot)
        .lineTo(ys, z_bot)
        .lineTo(ys, zt)
        .spline([(ys + 2, zt + 20), (ys + 20, zt + 41), (ys + 55, zt + 66),
                 (TRAP_END[0] + dy, TRAP_END[1])], includeCurrent=True)
        .lineTo(TRAP_END[0] + dy, z_top)
        .lineTo(y_front, z_top)
        .close()
    )


# ---------------------------------------------------------------------------
# Pedestal (tapered foot) with a low flange at the back
# ---------------------------------------------------------------------------
ped_ref = (PED_HW_BOT, PED_Y0_BOT, PED_Y1_BOT, PED_RF_BOT, PED_RB)
pedestal = loft([
    smooth_rrect_wire(PED_HW_BOT, PED_Y0_BOT, PED_Y1_BOT, PED_RF_BOT, PED_RB, 0.0, PED_PTS, ped_ref),
    smooth_rrect_wire(PED_HW_TOP, PED_Y0_TOP, PED_Y1_TOP, PED_RF_TOP, PED_RB, BOWL_BOTTOM_Z + 10,
                      PED_PTS, ped_ref),
])
flange = loft([
    rrect_wire(PED_HW_BOT - 3, 300.0, FLANGE_Y1, 20.0, PED_RB, 0.0),
    rrect_wire(PED_HW_BOT - 6, 300.0, FLANGE_Y1 - 3, 20.0, PED_RB - 3, FLANGE_H),
])

# ---------------------------------------------------------------------------
# Bowl (loft through foot / belly / rim sections)
# ---------------------------------------------------------------------------
bowl_sections = [
    # yc, a, bf, bb, z, nb   (rim follows the seat outline, wide at the back)
    (191.5, PED_HW_TOP - 2.5, 66.0, 90.0, BOWL_BOTTOM_Z, 2.0),
    (205.0, 150.0, 165.0, 200.0, 285.0, 1.9),
    (207.0, 169.0, 200.0, 280.0, 350.0, 1.7),
    (207.0, BOWL_A, 202.0, 320.0, RIM_Z, SEAT_NB),
]
bowl = loft([egg_wire(*s[:5], nb=s[5]) for s in bowl_sections], False)

# ---------------------------------------------------------------------------
# Neck (saddle between bowl, foot and deck) and trap column
# ---------------------------------------------------------------------------
NECK_TOP = RIM_Z - DECK_T + 1
neck_side = (
    cq.Workplane("YZ")
    .moveTo(240, 150)
    .lineTo(PED_Y1_TOP - 3, 150)
    .lineTo(PED_Y1_TOP - 3, 300)
    .spline([(PED_Y1_TOP - 1, 340), (NECK_BACK_TOP, NECK_TOP)], includeCurrent=True)
    .lineTo(240, NECK_TOP)
    .close()
    .extrude(DECK_HW + 10, both=True)
)
neck_front = (
    cq.Workplane("XZ")
    .moveTo(-NECK_HW, 150)
    .lineTo(NECK_HW, 150)
    .lineTo(NECK_HW, 240)
    .spline([(NECK_HW + 6, 300), (NECK_HW + 17, 340), (NECK_TOP_HW, NECK_TOP)],
            includeCurrent=True)
    .lineTo(-NECK_TOP_HW, NECK_TOP)
    .spline([(-NECK_HW - 17, 340), (-NECK_HW - 6, 300), (-NECK_HW, 240)],
            includeCurrent=True)
    .close()
    .extrude(-700)
)
neck = neck_side.intersect(neck_front)

# trap column behind the foot: block up to the top of the outlet socket
spine_side = (
    cq.Workplane("YZ")
    .moveTo(PED_Y1_TOP - 40, 0.0)
    .lineTo(SPINE_Y1, 0.0)
    .lineTo(SPINE_Y1, SPINE_TOP_Z)
    .lineTo(PED_Y1_TOP - 40, SPINE_TOP_Z + 30)
    .close()
    .extrude(SPINE_FRONT_HW + 10, both=True)
)
# in plan the trap column narrows from the foot width to the back face
spine_plan = (
    cq.Workplane("XY", origin=(0, 0, -10))
    .polyline([(-SPINE_FRONT_HW, 300.0), (SPINE_FRONT_HW, 300.0),
               (SPINE_FRONT_HW, PED_Y1_TOP - 8), (SPINE_HW, SPINE_Y1 - 6),
               (SPINE_HW, 700.0), (-SPINE_HW, 700.0),
               (-SPINE_HW, SPINE_Y1 - 6), (-SPINE_FRONT_HW, PED_Y1_TOP - 8)])
    .close()
    .extrude(RIM_Z + 20)
)
spine = spine_side.intersect(spine_plan)
spine = safe_fillet(spine, cq.selectors.BoxSelector((-120, PED_Y1_TOP - 12, SPINE_TOP_Z - 5),
                                                    (120, SPINE_Y1 + 1, SPINE_TOP_Z + 40)), RIB_R)
spine = safe_fillet(spine, cq.selectors.BoxSelector((-120, SPINE_Y1 - 8, -5),
                                                    (120, SPINE_Y1 + 1, SPINE_TOP_Z - 5)), 8.0)

# narrow trapway web sweeping up from the column to the underside of the deck
web = trap_profile(PED_Y1_TOP - 10, SPINE_TOP_Z - 30, NECK_TOP).extrude(WEB_HW, both=True)
web = safe_fillet(web, cq.selectors.BoxSelector((-60, SPINE_Y1 - 1, SPINE_TOP_Z - 1),
                                                (60, TRAP_END[0] + 1, TRAP_END[1] + 1)), WEB_HW - 4)

deck = (
    cq.Workplane("XY", origin=(0, 0, RIM_Z - DECK_T))
    .polyline([(-DECK_HW, 330.0), (DECK_HW, 330.0), (DECK_HW, DECK_FRONT_Y1),
               (DECK_BACK_HW, DECK_FRONT_Y1 + 25), (DECK_BACK_HW, DECK_Y1),
               (-DECK_BACK_HW, DECK_Y1), (-DECK_BACK_HW, DECK_FRONT_Y1 + 25),
               (-DECK_HW, DECK_FRONT_Y1)])
    .close()
    .extrude(DECK_T)
)
deck = safe_fillet(deck, "|Z", 10.0)
deck = safe_fillet(deck, lambda w: w.faces(">Z").edges(), 5.0)   # rounded nose on the deck edge

# ---------------------------------------------------------------------------
# Outlet horn (P-trap spigot)
# ---------------------------------------------------------------------------
horn = (
    cq.Workplane("XZ", origin=(0, SPINE_Y1 - 10, HORN_Z))
    .circle(HORN_D / 2)
    .extrude(-(HORN_Y1 - SPINE_Y1 + 10))
    .faces(">Y").edges().fillet(8.0)
)

# ---------------------------------------------------------------------------
# Flush valve housing under tank
# ---------------------------------------------------------------------------
valve = (
    cq.Workplane("XY", origin=(0, VALVE_Y, VALVE_Z0))
    .circle(VALVE_D / 2)
    .extrude(TANK_Z0 - VALVE_Z0 + 5)
    .faces("<Z").edges().fillet(8.0)
)

# ---------------------------------------------------------------------------
# Cistern
# ---------------------------------------------------------------------------
tank = loft([
    smooth_rrect_wire(TANK_HW_BOT, TANK_Y0 + 12, TANK_Y1, TANK_RF, TANK_RB, TANK_Z0),
    smooth_rrect_wire(TANK_HW_TOP, TANK_Y0, TANK_Y1, TANK_RF, TANK_RB, TANK_Z1),
])
tank = safe_fillet(tank, lambda w: w.faces("<Z").edges(), 6.0)

tank_lid = loft([
    smooth_rrect_wire(TANK_HW_TOP + 2, TANK_Y0 - 2, TANK_Y1 + 2, TANK_RF, TANK_RB, TANK_Z1 + 2),
    smooth_rrect_wire(TANK_HW_TOP + 2, TANK_Y0 - 2, TANK_Y1 + 2, TANK_RF, TANK_RB, LID_Z1),
])
tank_lid = safe_fillet(tank_lid, lambda w: w.faces(">Z").edges(), LID_EDGE_R)
lid_seam = loft([
    smooth_rrect_wire(TANK_HW_TOP - 3, TANK_Y0 + 3, TANK_Y1 - 3, TANK_RF - 3, TANK_RB, TANK_Z1 - 1),
    smooth_rrect_wire(TANK_HW_TOP - 3, TANK_Y0 + 3, TANK_Y1 - 3, TANK_RF - 3, TANK_RB, TANK_Z1 + 3),
])

# ---------------------------------------------------------------------------
# Seat ring and lid
# ---------------------------------------------------------------------------
cut_back = (cq.Workplane("XY").box(600, 600, 1000, centered=(True, False, False))
            .translate((0, SEAT_BACK, 0)))

SEAT_Z0 = RIM_Z + SEAT_GAP
seat = loft([
    egg_wire(SEAT_YC, SEAT_A - 3, SEAT_BF - 3, SEAT_BB - 3, SEAT_Z0, nb=SEAT_NB),
    egg_wire(SEAT_YC, SEAT_A, SEAT_BF, SEAT_BB, SEAT_Z0 + SEAT_T, nb=SEAT_NB),
])
seat = seat.cut(cut_back)


def egg_half_width(y, yc, a, bb, nb=2.0):
    t = min(1.0, max(0.0, (y - yc) / bb))
    return a * max(0.0, 1.0 - t ** nb) ** (1.0 / nb)


def corner_tool(r, a=SEAT_A, yc=SEAT_YC, bb=SEAT_BB, yb=SEAT_BACK, z0=RIM_Z - 5, h=120.0):
    """Material removed to round the two hinge-side corners of seat/lid in plan."""
    px = egg_half_width(yb, yc, a, bb, SEAT_NB)
    qx = egg_half_width(yb - 5.0, yc, a, bb, SEAT_NB)
    e1 = cq.Vector(-1, 0, 0)
    e2 = cq.Vector(qx - px, -5.0, 0).normalized()
    theta = math.acos(max(-1.0, min(1.0, e1.dot(e2))))
    d = r / math.tan(theta / 2)
    P = cq.Vector(px, yb, 0)
    T1 = P + e1 * d
    T2 = P + e2 * d
    bis = (e1 + e2).normalized()
    C = P + bis * (r / math.sin(theta / 2))
    M = C + (P - C).normalized() * r
    Pout = P + (P - C).normalized() * 20.0
    right = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(T1.x, T1.y)
        .threePointArc((M.x, M.y), (T2.x, T2.y))
        .lineTo(Pout.x + 10, T2.y)
        .lineTo(Pout.x + 10, yb + 10)
        .lineTo(T1.x, yb + 10)
        .close()
        .extrude(h)
    )
    return right.union(right.mirror("YZ"))


seat = seat.cut(corner_tool(SEAT_CORNER_R))
# opening of the seat ring (hidden under the closed lid)
seat_hole = cq.Workplane("XY").add(
    egg_solid(SEAT_HOLE[0], SEAT_HOLE[1], SEAT_HOLE[2], SEAT_HOLE[3], SEAT_Z0 - 1, SEAT_T + 2))
seat = seat.cut(seat_hole)

LID_Z0 = SEAT_Z0 + SEAT_T
lid = loft([
    egg_wire(SEAT_YC, SEAT_A, SEAT_BF, SEAT_BB, LID_Z0, nb=SEAT_NB),
    egg_wire(SEAT_YC, SEAT_A - LID_INSET, SEAT_BF - LID_INSET, SEAT_BB - LID_INSET,
             LID_Z0 + LID_T, nb=SEAT_NB),
])
lid = lid.cut(cut_back)
lid = lid.cut(corner_tool(SEAT_CORNER_R))
lid = safe_fillet(lid, lambda w: w.faces(">Z").edges(), 4.0)
# short parting groove on the lid centre line at the hinge end
lid_groove = (
    cq.Workplane("XY", origin=(0, SEAT_BACK - 12 - LID_GROOVE_L / 2, LID_Z0 + LID_T - 1.5))
    .rect(2.0, LID_GROOVE_L)
    .extrude(5.0)
)
lid = lid.cut(lid_groove)

# seat spacer (hinge block ties seat to rim)
hinge = (
    cq.Workplane("XY", origin=(0, SEAT_BACK - 22, RIM_Z - 2))
    .rect(190, 36)
    .extrude(SEAT_GAP + SEAT_T + 4)
)

# ---------------------------------------------------------------------------
# Assemble
# ---------------------------------------------------------------------------
body = pedestal
for part in (flange, bowl, neck, spine, web, deck):
    body = fuse(body, part)
# ---------------------------------------------------------------------------
# Bowl cavity (flushing well, under the closed seat)
# ---------------------------------------------------------------------------
cavity = loft([egg_wire(*c[:4], c[4]) for c in BOWL_CAVITY], False)
body = body.cut(cavity)
for part in (horn, valve, tank, lid_seam, tank_lid, hinge, seat, lid):
    body = fuse(body, part)

result = body
